import math
import cadquery as cq

# =====================================================================
#  Architectural massing model (hollow shell, open underside)
#  X: 0..100 (left->right), Y: 0..116 (front->back), Z: 0..77 (up)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
LX, LY, LZ = 100.0, 116.0, 77.0     # overall envelope
WALL = 2.0                           # shell wall thickness
BASE = -6.0                          # silhouettes start below the floor (cut at z=0)

# facade: 45 deg stepped plane (x + z = FAC_C) made of tilted bands with arched boundaries
SLOPE = 45.0                         # facade slope from horizontal
FAC_C = 97.5                         # facade reference plane  x + z = FAC_C
BAND_TILT = 8.0                      # each band is this much steeper than the facade (sawtooth)
# band boundaries given as three (y, z) points of an arc on the facade plane (top -> bottom)
ARC_AB = [(47.8, 57.7), (71.2, 48.7), (93.8, 51.7)]
ARC_BC = [(36.5, 47.2), (69.7, 38.9), (104.4, 40.4)]
ARC_CD = [(42.6, 37.4), (69.7, 31.3), (99.9, 32.9)]
# bands: (y from, y to, upper arc, lower arc)
BANDS = [(49.0, 106.0, None, ARC_AB), (42.0, 106.0, ARC_AB, ARC_BC),
         (37.0, 104.0, ARC_BC, ARC_CD), (38.0, 99.0, ARC_CD, None)]

# wing: box rotated 45 deg about Y sitting on the facade
WING_TOP = 135.5                     # top face plane   x + z
WING_END = 64.5                      # end face plane   x - z
WING_BOT = 101.0                     # bottom face plane x + z

# lower front block and the tall mass behind it
FR_Z, FR_SY = 36.0, 0.20             # low roof height and rise towards the back
TALL_Y = 25.0                        # vertical front face of the tall mass
RIDGE_Z, RIDGE_K = 57.0, 0.87        # sloped facet above it: z = RIDGE_Z + RIDGE_K * (y - TALL_Y)
FR_XR, FR_ZR, FR_KR, FR_YR = 49.0, 48.0, 0.30, 24.5   # front-right block roof z = FR_ZR + FR_KR*y (y < FR_YR)
# left face of the peak: z <= PL_Z0 + PL_KX * (x - 10) + PL_KY * (y - 25)
PL_Z0, PL_KX, PL_KY = 50.5, 1.01, 0.447
# left wall eaves (y < LW_Y1): z <= LW_Z0 + LW_KX * x + LW_KY * y
LW_Z0, LW_KX, LW_KY, LW_Y1 = 40.3, 2.0, -0.13, 60.0

V = cq.Vector


# ---------------- helpers ----------------
def poly_face(pts3):
    return cq.Face.makeFromWires(cq.Wire.makePolygon([V(*p) for p in pts3], close=True))


def offset_poly(pts, off):
    """inward 2D offset of a closed polygon (list of (u, v)), sharp corners"""
    if off <= 0:
        return pts
    w = cq.Wire.makePolygon([V(u, v, 0) for u, v in pts], close=True)
    w2 = w.offset2D(-off, kind="intersection")[0]
    out = []
    for e in w2.Edges():
        p = e.startPoint()
        out.append((p.x, p.y))
    return out


def prism_xz(pts, y0, y1, off=0.0):
    """polygon in (x, z), extruded along +Y"""
    q = offset_poly(pts, off)
    f = poly_face([(x, y0, z) for x, z in q])
    return cq.Solid.extrudeLinear(f, V(0, y1 - y0, 0))


def prism_yz(pts, x0, x1, off=0.0):
    """polygon in (y, z), extruded along +X"""
    q = offset_poly(pts, off)
    f = poly_face([(x0, y, z) for y, z in q])
    return cq.Solid.extrudeLinear(f, V(x1 - x0, 0, 0))


def prism_xy(pts, z0, z1, off=0.0):
    """polygon in (x, y), extruded along +Z"""
    q = offset_poly(pts, off)
    f = poly_face([(x, y, z0) for x, y in q])
    return cq.Solid.extrudeLinear(f, V(0, 0, z1 - z0))


def box_pts(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0, V(x0, y0, z0))


def halfspace(origin, normal, size=600.0):
    """big block lying on the plane through origin, on the side the normal points to"""
    n = V(*normal).normalized()
    ref = V(0, 0, 1) if abs(n.z) < 0.9 else V(1, 0, 0)
    xd = ref.cross(n).normalized()
    pl = cq.Plane(origin=V(*origin), xDir=xd, normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(size).val()


def halfspace_off(origin, normal, off):
    """half-space shifted by 'off' against its normal (dilated cutter)"""
    n = V(*normal).normalized()
    return halfspace(V(*origin) - n * off, normal)


def obox(center, size, rot=(0.0, 0.0, 0.0), off=0.0):
    """box (dx,dy,dz) centred at center, rotated about its centre (deg, X then Y then Z)"""
    sx, sy, sz = (s - 2 * off for s in size)
    b = cq.Solid.makeBox(sx, sy, sz, V(-sx / 2, -sy / 2, -sz / 2))
    o = V(0, 0, 0)
    for ax, ang in zip((V(1, 0, 0), V(0, 1, 0), V(0, 0, 1)), rot):
        if ang:
            b = b.rotate(o, ax, ang)
    return b.translate(V(*center))


# ---------------- silhouettes (front X-Z, side Y-Z, plan X-Y) ----------------
FRONT = [(0, BASE), (0, 36.5), (6.2, 48.9), (14, 65.6), (19.7, 71.9), (26, 76.5), (35.4, 77),
         (40.6, 71.9), (47.9, 66.7), (52, 61.4), (56.6, 65.4), (67.6, 68.2), (84, 54),
         (100, 35.5), (81.8, 20.5), (93.8, 12.6), (95.8, 9.5), (95.8, BASE)]

SIDE = [(0.4, BASE), (0.4, 47.7), (3, 49.1), (13.3, 50.6), (24.2, 55.8), (31.7, 65.2),
        (38.8, 67.1), (39.7, 69.4), (48.7, 77.0), (53.1, 75), (58.7, 71.3), (65.4, 69.4),
        (76.6, 68.5), (84.2, 70.4), (94.6, 73.2), (97.4, 72.7), (105.9, 67.5),
        (105.9, 52.5), (114.4, 50.6), (116, 48.7), (116, BASE)]

TOP = [(35.8, 0), (59.6, 1.1), (74.3, 5.2), (76.6, 10.8), (76.6, 24), (99, 23.1),
       (100, 35.5), (96.4, 39.5), (87, 57.6), (85, 70), (87.3, 82), (90.4, 89.4),
       (82, 99), (70.6, 99), (68, 102.6), (60.8, 105), (57.3, 111), (55.4, 112.9),
       (50, 116), (39, 116), (24, 106), (15, 96.7), (11.7, 87.4), (10, 78.3), (10, 72.3),
       (13.6, 57.3), (8.7, 48.2), (0, 32.8), (6.3, 6.3), (12, 2.3)]

WING_XY = [(63.2, 24.0), (60.0, 52.5), (75.8, 53.2), (78.3, 48.6), (88.4, 47.6),
           (90.4, 40.7), (100.0, 35.2), (99.7, 20.8)]

HEAD_BOXES = [
    # centre, size, rotations (x, y, z) -- front face carries a window
    ((22.0, 22.0, 49.5), (14.5, 10.0, 17.0), (0.0, 6.0, -12.0)),     # left dormer
    ((40.5, 24.0, 44.0), (14.0, 10.0, 11.5), (0.0, 0.0, 0.0)),       # middle dormer
    ((41.3, 8.5, 29.8), (12.0, 17.0, 16.0), (0.0, 0.0, 0.0)),        # lower bay at the front
    ((56.0, 31.0, 56.0), (13.0, 12.0, 13.0), (-15.0, 0.0, -25.0)),   # right tilted box
]

# screw bosses inside the rim: (x, y)
BOSSES = [(13.5, 7.0), (64.0, 5.0), (88.5, 34.0), (83.5, 89.5), (44.5, 112.0),
          (16.5, 89.5), (14.5, 51.0)]
BOSS_D, BOSS_H, BOSS_HOLE = 6.0, 9.0, 2.0

# door openings with a thin surround: (centre x, y), outward wall normal (x, y), width, height
DOORS = [((31.5, 110.3), (-0.555, 0.832), 8.0, 17.0),      # back-left entrance
         ((58.4, 108.9), (0.864, 0.504), 3.0, 7.0)]        # small service door, back-right
DOOR_FRAME, DOOR_PROUD, DOOR_RECESS = 1.2, 0.8, 1.0

ca, sa = math.cos(math.radians(SLOPE)), math.sin(math.radians(SLOPE))
AX = V(ca, 0, -sa)          # down-slope direction
NR = V(sa, 0, ca)           # outward facade normal
VA = V(-ca, 0, sa)          # up-slope direction (local v of the facade plane)
FZ0 = 66.8                  # facade plane origin height at x = FAC_C - FZ0
O_F = V(FAC_C - FZ0, 0, FZ0)
F_PLANE = cq.Plane(origin=O_F, xDir=V(0, 1, 0), normal=NR)


def zv(z):
    """height on the facade plane -> local v (up-slope)"""
    return (z - FZ0) / sa


def arc_fit(pts):
    """circle through three (y, z) facade points, in (u, v) facade coordinates"""
    (x1, y1), (x2, y2), (x3, y3) = [(u, zv(z)) for u, z in pts]
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    ux = ((x1 ** 2 + y1 ** 2) * (y2 - y3) + (x2 ** 2 + y2 ** 2) * (y3 - y1) + (x3 ** 2 + y3 ** 2) * (y1 - y2)) / d
    uy = ((x1 ** 2 + y1 ** 2) * (x3 - x2) + (x2 ** 2 + y2 ** 2) * (x1 - x3) + (x3 ** 2 + y3 ** 2) * (x2 - x1)) / d
    r = math.hypot(x1 - ux, y1 - uy)
    return ux, uy, r


def arc_v(arc, u):
    cx, cy, r = arc_fit(arc)
    dv = math.sqrt(max(r * r - (u - cx) ** 2, 0.0))
    return cy - dv if arc[1][1] < arc[0][1] else cy + dv


def band_mid_v(band):
    y0, y1, up, lo = BANDS[band]
    um = 0.5 * (y0 + y1)
    vt = arc_v(up, um) if up else zv(69.0)
    vb = arc_v(lo, um) if lo else zv(6.0)
    return 0.5 * (vt + vb)


def band_normal():
    a = math.radians(SLOPE + BAND_TILT)
    return V(math.sin(a), 0, math.cos(a))


def band_cutter(band, off=0.0):
    """everything outside the (tilted) band surface, over the band's arched strip"""
    y0, y1, up, lo = BANDS[band]
    um = 0.5 * (y0 + y1)
    far = 120.0
    wp = cq.Workplane(F_PLANE).workplane(offset=-60.0)
    if up:
        wp = wp.moveTo(y0, arc_v(up, y0)).threePointArc((up[1][0], zv(up[1][1])), (y1, arc_v(up, y1)))
    else:
        wp = wp.moveTo(y0, far).lineTo(y1, far)
    if lo:
        wp = wp.lineTo(y1, arc_v(lo, y1)).threePointArc((lo[1][0], zv(lo[1][1])), (y0, arc_v(lo, y0)))
    else:
        wp = wp.lineTo(y1, -far).lineTo(y0, -far)
    w = wp.close().wire().val()
    if off > 0:
        w = w.offset2D(off, kind="arc")[0]
    f = cq.Face.makeFromWires(w)
    prism = cq.Solid.extrudeLinear(f, NR * 160.0)
    # outward side of the band plane (through the band mid-line, steeper than the facade)
    pm = O_F + VA * band_mid_v(band) + V(0, um, 0)
    return prism.intersect(halfspace_off(pm, band_normal(), off))


def band_point(band, y, z):
    """point on band surface at facade position (y, z)"""
    v = zv(z)
    t = (v - band_mid_v(band)) * math.tan(math.radians(BAND_TILT))
    return O_F + V(0, y, 0) + VA * v + NR * t


def build(off):
    """solid massing; off > 0 gives the inward-offset (cavity) version"""
    front_prism = prism_xz(FRONT, -5, LY + 5, off)
    side_prism = prism_yz(SIDE, -5, LX + 5, off)
    body = front_prism.intersect(side_prism).intersect(prism_xy(TOP, BASE, LZ + 5, off))

    # low front roof + steep front face of the tall mass
    cut_l = halfspace_off((0, 0, FR_Z), (0, -FR_SY, 1.0), off)
    cut_l = cut_l.intersect(box_pts(-10, FR_XR + off, -10, TALL_Y + off, -10, 100))
    facet = halfspace_off((0, TALL_Y, RIDGE_Z), (0, -RIDGE_K, 1.0), off)
    facet = facet.intersect(box_pts(-10, FR_XR + off, -10, 60, -10, 100))
    cut_l = cut_l.fuse(facet)
    cut_r = halfspace_off((FR_XR, 0, FR_ZR), (0, -FR_KR, 1.0), off)
    cut_r = cut_r.intersect(box_pts(FR_XR - off, 80, -10, FR_YR + off, -10, 100))
    body = body.cut(cut_l.fuse(cut_r))
    body = body.cut(halfspace_off((10.0, 25.0, PL_Z0), (-PL_KX, -PL_KY, 1.0), off))
    eaves = halfspace_off((0.0, 0.0, LW_Z0), (-LW_KX, -LW_KY, 1.0), off)
    body = body.cut(eaves.intersect(box_pts(-10, 40, 20, LW_Y1 + off, -10, 100)))

    # stepped facade bands
    for band in range(len(BANDS)):
        body = body.cut(band_cutter(band, off))

    # wing
    wing = prism_xy(WING_XY, BASE, LZ + 5, off)
    slab_len = 200.0
    th = (WING_TOP - WING_BOT) / math.sqrt(2) - 2 * off
    slab = cq.Solid.makeBox(slab_len, 120, th, V(0, 0, 0)).rotate(V(0, 0, 0), V(0, 1, 0), 45)
    ex = (WING_BOT + WING_END) / 2.0
    ez = (WING_BOT - WING_END) / 2.0
    corner = V(ex, 0, ez) + NR * off - AX * off
    slab = slab.translate(corner - AX * slab_len + V(0, -10, 0))
    wing = wing.intersect(slab).intersect(front_prism).intersect(side_prism)
    body = body.fuse(wing)

    # head cluster boxes (clipped to the silhouettes)
    for c, s, r in HEAD_BOXES:
        b = obox(c, s, r, off).intersect(front_prism).intersect(side_prism)
        body = body.fuse(b)
    return body.clean()


outer = build(0.0).intersect(box_pts(-5, LX + 5, -5, LY + 5, 0, LZ + 5))
inner = build(WALL)
shell = outer.cut(inner)


# ---------------- windows ----------------
WIN_W, WIN_H = 10.0, 11.0            # facade window opening (across, along the band)
FAC_WINDOWS = [                       # (band, (y, z) centres measured on the facade)
    (0, [(55.0, 70.5), (70.5, 64.5), (89.3, 66.0)]),
    (0, [(55.0, 60.0), (70.5, 53.9), (89.3, 55.5)]),
    (1, [(62.9, 48.7), (80.3, 42.7), (99.1, 44.9)]),
    (2, [(57.6, 38.1), (75.0, 34.3), (93.8, 35.9)]),
    (3, [(46.3, 29.1), (63.6, 23.8), (81.8, 24.5)]),
    (3, [(46.3, 16.2), (63.6, 11.0), (81.8, 12.5)]),
]


def cutter(origin, xdir, normal, w, h, depth=12.0):
    pl = cq.Plane(origin=origin, xDir=xdir, normal=normal)
    return cq.Workplane(pl).workplane(offset=-depth / 2).rect(w, h).extrude(depth).val()


def rot_vec(v, rr):
    e = cq.Edge.makeLine(V(0, 0, 0), v)
    for ax, ang in zip((V(1, 0, 0), V(0, 1, 0), V(0, 0, 1)), rr):
        if ang:
            e = e.rotate(V(0, 0, 0), ax, ang)
    return e.endPoint() - e.startPoint()


windows = []
for band, pts in FAC_WINDOWS:
    for y, z in pts:
        windows.append(cutter(band_point(band, y, z), V(0, 1, 0), band_normal(), WIN_W, WIN_H))

# skylights on the low front roof: (centre, normal, w, h)
SKYLIGHTS = [
    ((20.0, 11.0, 38.2), V(0, -0.35, 1), 8.0, 8.0),
    ((40.4, 14.5, 39.0), V(0, -0.35, 1), 7.0, 6.0),
    ((57.0, 11.0, 51.3), V(0, -0.30, 1), 7.0, 7.0),
]
for c, nrm, w, h in SKYLIGHTS:
    windows.append(cutter(V(*c), V(1, 0, 0), nrm, w, h, depth=6.0))

# windows in the front faces of the dormer boxes (follow the box rotation)
DORMER_WIN = [(9.0, 9.5), (8.5, 6.5), (0, 0), (9.0, 8.0)]
for (c, s, r), (w, h) in zip(HEAD_BOXES, DORMER_WIN):
    if w <= 0:
        continue
    xd, nd = rot_vec(V(1, 0, 0), r), rot_vec(V(0, -1, 0), r)
    p = V(*c) + nd * (s[1] / 2)
    windows.append(cutter(p, xd, nd, w, h, depth=2 * WALL + 4))

for wc in windows:
    shell = shell.cut(wc)

# doors: recessed leaf plus a proud surround
for (dx, dy), (nx, ny), dw, dh in DOORS:
    n = V(nx, ny, 0).normalized()
    xd = V(0, 0, 1).cross(n).normalized()
    pl = cq.Plane(origin=V(dx, dy, dh / 2), xDir=xd, normal=n)
    frame = (cq.Workplane(pl).rect(dw + 2 * DOOR_FRAME, dh + 2 * DOOR_FRAME).extrude(DOOR_PROUD).val()
             .cut(cq.Workplane(pl).workplane(offset=-1).rect(dw, dh).extrude(DOOR_PROUD + 2).val()))
    frame = frame.intersect(box_pts(-5, LX + 5, -5, LY + 5, 0, LZ))
    shell = shell.fuse(frame)
    # recessed door leaf (half the wall thickness)
    shell = shell.cut(cq.Workplane(pl).workplane(offset=-DOOR_RECESS).rect(dw, dh)
                      .extrude(DOOR_RECESS + 3).val())

# screw bosses: vertical pins with a domed top, tied to the nearest wall, drilled from below
for bx, by in BOSSES:
    pin = cq.Solid.makeCylinder(BOSS_D / 2, BOSS_H, V(bx, by, 0), V(0, 0, 1))
    pin = pin.fuse(cq.Solid.makeSphere(BOSS_D / 2, V(bx, by, BOSS_H), angleDegrees1=0, angleDegrees2=90))
    pin = pin.intersect(outer)
    shell = shell.fuse(pin)
    shell = shell.cut(cq.Solid.makeCylinder(BOSS_HOLE / 2, BOSS_H * 0.8, V(bx, by, -0.1), V(0, 0, 1)))
shell = shell.clean()

# keep the main body only (guards against slivers from tangent cuts)
solids = sorted(shell.Solids(), key=lambda s: s.Volume(), reverse=True)
result = cq.Workplane("XY").add(solids[0])
